import cadquery as cq

# ---- driving dimensions (mm) ----
L = 480.0          # base plate length (X)
W = 102.0          # base / end plate width (Y)
H = 99.0           # overall height of end plates (measured from underside of base)
T_BASE = 9.0       # base plate thickness
T_PLATE = 9.0      # end plate thickness (same stock as the base)
INSET = 15.0       # distance from base end to outer face of end plate
HOLE_D = 12.0      # bolt hole diameter
HOLE_PITCH = 60.0  # square hole pattern pitch (Y and Z), centred on each end plate

# base plate, centred in X/Y, bottom at z=0
base = cq.Workplane("XY").box(L, W, T_BASE, centered=(True, True, False))


def end_plate(sign):
    """Upright end plate (full height, running down through the base)
    with a 2x2 square pattern of through holes.
    sign = -1 -> plate at the -X end, +1 -> plate at the +X end."""
    xc = sign * (L / 2 - INSET - T_PLATE / 2)
    plate = (cq.Workplane("XY")
             .box(T_PLATE, W, H, centered=(True, True, False))
             .translate((xc, 0, 0)))
    # sketch plane normal to X; local x runs along +Z so the cylinder seam
    # of each hole sits at its top (out of sight, as on the original)
    hole_plane = cq.Plane(origin=(xc - T_PLATE, 0, H / 2),
                          xDir=(0, 0, 1), normal=(1, 0, 0))
    holes = (cq.Workplane(hole_plane)
             .rarray(HOLE_PITCH, HOLE_PITCH, 2, 2)
             .circle(HOLE_D / 2)
             .extrude(2 * T_PLATE))
    return plate.cut(holes)


left = end_plate(-1)
right = end_plate(+1)

# Fuse without merging coplanar faces, so the seams of the end plates that
# run down through the base stay visible, as on the original part.
result = base.union(left, clean=False).union(right, clean=False)
